import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Square wall-mount enclosure base (open at the front, -Y; back plate at +Y)
# ---------------------------------------------------------------------------
W = 86.0          # outer width  (X)
H = 86.0          # outer height (Z)
D = 22.8          # outer depth  (Y)
R_OUT = 9.6       # outer corner radius (XZ)
WALL = 2.8        # side wall thickness
BACK_T = 5.1      # back plate thickness
R_FRONT_O = 2.5   # front rim outer fillet
R_FRONT_I = 0.0   # front rim inner fillet (0 = sharp)
R_BACK = 2.6      # back outer edge fillet

Y_PL = D - BACK_T             # inner surface of back plate
HX = W / 2.0 - WALL           # inner half width
HZ = H / 2.0 - WALL           # inner half height
R_IN = R_OUT - WALL

# windows (two, mirrored about X=0)
WIN_X0 = 8.3                  # inner edge of window (|X|)
WIN_HZ = 13.45                # half height of opening
FRAME_T = 1.2                 # frame wall thickness
FRAME_H = 3.4                 # frame protrusion above back plate

# raised strip on the left side of the back plate
STRIP_X = -26.2
STRIP_H = 0.9

# tall pads
PAD_H = 7.1
TL_PAD = (-24.4, -9.2, 27.6)  # x0, x1, z0 (runs to top wall)
TL_HOLE = (-17.0, 31.8, 3.1)
CP_X0 = 25.0                  # right corner pads
CP_Z0 = 24.8
CP_R = 8.3
CP_HOLE = (32.0, 31.8, 3.3)
PAD_HOLE_DEPTH = 8.0

# small screw bosses
BOSS_R = 3.5
BOSS_HOLE_R = 1.9
BOSS_H = FRAME_H   # flush with the window frames
BOSSES = [(-13.9, 17.0), (4.2, 28.8), (27.7, -15.9), (-10.4, -22.4)]

# hexagon alignment marks
HEX_R = 3.4
HEX_D = 0.4       # hexagon recess depth
TRI_R = 2.4
TRI_H = 1.0       # raised triangle height above the recess floor
HEXES = [(-16.8, 23.5, 90.0), (24.8, 24.7, 44.6), (24.8, -24.8, -44.0)]

# side slots in the -X wall
SLOT_Y = 13.2
SLOT_W = 5.0
SLOT_L = 17.5
SLOT_Z = 24.0
SLOT_R = 1.2

# logo on +X wall
LOGO_Y = 11.5
LOGO_Z = 1.0
LOGO_R = 7.6
ENGRAVE = 0.35


def xz(y0, x=0.0, z=0.0):
    """Workplane parallel to XZ at Y=y0 (local x->X, local y->Z).
    Extrude with a negative distance to grow toward +Y."""
    return cq.Workplane("XZ", origin=(x, y0, z))


def box(x0, x1, z0, z1, y0, y1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_y(cx, cz, r, y0, y1):
    return xz(y0, cx, cz).circle(r).extrude(-(y1 - y0))


def rr_sd(x, z, hx, hz, r):
    qx = abs(x) - (hx - r)
    qz = abs(z) - (hz - r)
    out = math.hypot(max(qx, 0.0), max(qz, 0.0))
    ins = min(max(qx, qz), 0.0)
    return out + ins - r


def pick_edges(shape, pred):
    res = []
    for e in shape.Edges():
        pts = [e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0)]
        if all(pred(p) for p in pts):
            res.append(e)
    return res


# ---------------- main shell ----------------
outer = (xz(0.0).sketch().rect(W, H).vertices().fillet(R_OUT).finalize()
         .extrude(-D))
outer = outer.faces(">Y").edges().fillet(R_BACK)
cavity = (xz(-1.0).sketch().rect(2 * HX, 2 * HZ).vertices().fillet(R_IN)
          .finalize().extrude(-(Y_PL + 1.0)))
shell = outer.cut(cavity).val()

if R_FRONT_I > 0:
    inner_front = pick_edges(
        shell, lambda p: abs(p.y) < 1e-4 and abs(rr_sd(p.x, p.z, HX, HZ, R_IN)) < 1e-3)
    shell = shell.fillet(R_FRONT_I, inner_front)
outer_front = pick_edges(
    shell, lambda p: abs(p.y) < 1e-4 and abs(rr_sd(p.x, p.z, W / 2, H / 2, R_OUT)) < 1e-3)
shell = shell.fillet(R_FRONT_O, outer_front)
body = cq.Workplane("XY").add(shell)

# ---------------- back plate features ----------------
EPS = 0.3
feat = None


def add(a, b):
    return b if a is None else a.union(b)


# raised strip (left side)
feat = add(feat, box(-HX - EPS, STRIP_X, -HZ - EPS, HZ + EPS, Y_PL - STRIP_H, Y_PL + EPS))

# window frames (3-sided, against the side walls)
for s in (-1, 1):
    fx0 = WIN_X0 - FRAME_T
    frame = box(fx0, HX + EPS, -WIN_HZ - FRAME_T, WIN_HZ + FRAME_T,
                Y_PL - FRAME_H, Y_PL + EPS)
    if s < 0:
        frame = frame.mirror("YZ")
    feat = add(feat, frame)

# top-left tall pad
x0, x1, z0 = TL_PAD
tl = (xz(Y_PL - PAD_H, (x0 + x1) / 2, (z0 + HZ + EPS) / 2)
      .sketch().rect(x1 - x0, HZ + EPS - z0).vertices("<Y").fillet(1.0).finalize()
      .extrude(-(PAD_H + EPS)))
feat = add(feat, tl)

# right corner pads (top & bottom)
for sz in (1, -1):
    w = HX + EPS - CP_X0
    h = HZ + EPS - CP_Z0
    cp = (xz(Y_PL - PAD_H, CP_X0 + w / 2, sz * (CP_Z0 + h / 2))
          .sketch().rect(w, h)
          .vertices("<X and <Y" if sz > 0 else "<X and >Y").fillet(CP_R)
          .finalize().extrude(-(PAD_H + EPS)))
    feat = add(feat, cp)

# screw bosses
for (bx, bz) in BOSSES:
    feat = add(feat, cyl_y(bx, bz, BOSS_R, Y_PL - BOSS_H, Y_PL + EPS))

# keep all interior features inside the wall envelope
clip = (xz(0.0).sketch().rect(2 * HX + 0.4, 2 * HZ + 0.4).vertices().fillet(R_IN + 0.2)
        .finalize().extrude(-(Y_PL + 1.0)))
feat = feat.intersect(clip)
body = body.union(feat)

# small root fillets on the free-standing screw bosses
BOSS_ROOT_R = 0.6
try:
    roots = []
    for (bx, bz) in BOSSES:
        if abs(bz) > WIN_HZ + FRAME_T + BOSS_R:   # not merged into a window frame
            roots += pick_edges(
                body.val(),
                lambda p, bx=bx, bz=bz: abs(p.y - Y_PL) < 1e-3
                and abs(math.hypot(p.x - bx, p.z - bz) - BOSS_R) < 1e-3)
    if roots:
        body = cq.Workplane("XY").add(body.val().fillet(BOSS_ROOT_R, roots))
except Exception:
    pass

# ---------------- cuts ----------------
# windows through the back
for s in (-1, 1):
    win = box(WIN_X0, HX + 0.01, -WIN_HZ, WIN_HZ, Y_PL - FRAME_H - 1, D + 1)
    if s < 0:
        win = win.mirror("YZ")
    body = body.cut(win)

# boss through holes
for (bx, bz) in BOSSES:
    body = body.cut(cyl_y(bx, bz, BOSS_HOLE_R, Y_PL - BOSS_H - 1, D + 1))

# pad blind holes
hx_, hz_, hr = TL_HOLE
body = body.cut(cyl_y(hx_, hz_, hr, Y_PL - PAD_H - 1, Y_PL - PAD_H + PAD_HOLE_DEPTH))
for sz in (1, -1):
    hx_, hz_, hr = CP_HOLE
    body = body.cut(cyl_y(hx_, sz * hz_, hr, Y_PL - PAD_H - 1, Y_PL - PAD_H + PAD_HOLE_DEPTH))

# hexagon recesses with raised triangular arrows (pointing at the screw holes)
for (hx_, hz_, ang) in HEXES:
    hexr = (xz(Y_PL - 1.0, hx_, hz_).transformed(rotate=(0, 0, ang))
            .polygon(6, 2 * HEX_R).extrude(-(1.0 + HEX_D)))
    body = body.cut(hexr)
    tri = (xz(Y_PL + HEX_D - TRI_H, hx_, hz_).transformed(rotate=(0, 0, ang))
           .polygon(3, 2 * TRI_R).extrude(-(TRI_H + 0.05)))
    body = body.union(tri)

# slots through the -X wall
for sz in (1, -1):
    slot = (cq.Workplane("YZ", origin=(-W / 2 - 1, SLOT_Y, sz * SLOT_Z))
            .sketch().rect(SLOT_W, SLOT_L).vertices().fillet(SLOT_R).finalize()
            .extrude(WALL + 2))
    body = body.cut(slot)

# engraved logo on +X wall: arc + "TII" bars
arc_outer = cq.Workplane("YZ", origin=(W / 2 - ENGRAVE, LOGO_Y, LOGO_Z)).circle(LOGO_R + 0.3).extrude(2)
arc_inner = cq.Workplane("YZ", origin=(W / 2 - ENGRAVE - 1, LOGO_Y, LOGO_Z)).circle(LOGO_R - 0.3).extrude(4)
lower = box(W / 2 - 2, W / 2 + 2, LOGO_Z - LOGO_R - 1, LOGO_Z, LOGO_Y - LOGO_R - 1, LOGO_Y + LOGO_R + 1)
arc = arc_outer.cut(arc_inner).intersect(lower)
body = body.cut(arc)
for (y0, y1, z0, z1) in [(8.5, 14.2, 3.0, 4.6),     # T stem
                         (12.9, 14.4, 2.0, 6.2),    # T bar
                         (8.5, 14.4, -0.5, 1.0),    # I
                         (8.5, 14.4, -3.4, -1.9)]:  # I
    body = body.cut(box(W / 2 - ENGRAVE, W / 2 + 1, z0, z1, y0, y1))

# recessed label fields on the back face
LBL_DEPTH = 0.5
LABELS = [(14.8, 33.2, 16.5, 38.5, "88V", 11.0),
          (-8.6, 1.2, 16.5, 38.5, "PG1", 9.0),
          (-26.9, -17.4, 16.5, 38.0, "IN2", 9.0),
          (14.5, 25.7, -38.5, -18.0, "OUT", 8.5),
          (-23.9, -12.5, -38.5, -16.8, "PG3", 9.0)]
for (x0, x1, z0, z1, _t, _fs) in LABELS:
    lbl = (xz(D - LBL_DEPTH, (x0 + x1) / 2, (z0 + z1) / 2)
           .sketch().rect(x1 - x0, z1 - z0).vertices().fillet(1.5).finalize()
           .extrude(-(LBL_DEPTH + 1)))
    body = body.cut(lbl)

# small recessed rings around the boss holes on the back face
for (bx, bz) in BOSSES:
    body = body.cut(cyl_y(bx, bz, BOSS_HOLE_R + 0.6, D - LBL_DEPTH, D + 1))

# screw symbols next to the windows
for (sx_, sz_) in [(34.5, -17.9), (-35.9, 18.3)]:
    body = body.cut(cyl_y(sx_, sz_, 1.8, D - LBL_DEPTH, D + 1))

# raised lettering inside the label fields (reads top-to-bottom seen from the back)
try:
    for (x0, x1, z0, z1, txt, fs) in LABELS:
        pl = cq.Plane(origin=((x0 + x1) / 2, D - LBL_DEPTH - 0.05, (z0 + z1) / 2),
                      xDir=(0, 0, -1), normal=(0, 1, 0))
        letters = cq.Workplane(pl).text(txt, fs, LBL_DEPTH - 0.05, combine=False)
        if letters.solids().size() > 0:
            body = body.union(letters)
except Exception:
    pass

result = body
